import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
R = 20.0            # outer radius of the flanges
T = 10.6            # total thickness (along Y)
GROOVE_D = 2.85     # depth of the V groove (radial)
EDGE_FIL = 0.75     # fillet on the outer face edges

CENTER_HOLE_D = 2.2     # small centre hole (through)
TIE_HOLE_D = 3.5        # string/tie hole (through)
TIE_HOLE_R = 14.25      # radial position of tie hole (towards +Z)
SLOT_FIL = 0.6          # fillet on the slot edges
SLOT_W = 1.5            # slot from tie hole to rim, through back half

CROSS_DEPTH = 2.4       # servo-horn cross recess in back face
CROSS_L = 13.8          # centre to arm tip (outer extent)
CROSS_TIP_R = 2.2       # arm tip radius
CROSS_BASE_HW = 3.7     # arm half width at centre
CROSS_CORNER_FIL = 0.6   # fillet in the concave corners of the cross
CROSS_ANGLE0 = 45.0     # first arm angle (deg, measured in XZ plane from +X)

VIEW = {"azimuth": 45, "elevation": 26}


def _safe_fillet(wp, edges, radius):
    """Fillet `edges`; fall back to smaller radii (or none) if the kernel
    returns an invalid solid, so the part is always a clean B-rep."""
    if radius <= 0 or not edges:
        return wp
    for k in (1.0, 0.8, 0.6, 0.4):
        try:
            out = wp.newObject(edges).fillet(radius * k)
            v = out.val()
            if v.isValid() and len(v.Solids()) == 1:
                return out
        except Exception:
            pass
    return wp


# ---------------- body: revolved V-groove pulley ----------------
# profile in (r, y); revolve around the Y axis
h = T / 2.0
pts = [
    (0.0, -h),
    (R, -h),
    (R - GROOVE_D, 0.0),
    (R, h),
    (0.0, h),
]
body = (
    cq.Workplane("XY")
    .polyline(pts)
    .close()
    .revolve(360.0, (0, 0, 0), (0, 1, 0))
)
# round the two outer rim edges (circles at r=R)
rim_edges = [
    e for e in body.edges().vals()
    if e.geomType() == "CIRCLE" and abs(e.radius() - R) < 1e-6
]
body = _safe_fillet(body, rim_edges, EDGE_FIL)

# ---------------- holes ----------------
center_hole = (
    cq.Workplane("XZ")
    .circle(CENTER_HOLE_D / 2.0)
    .extrude(T, both=True)
)
tie_hole = (
    cq.Workplane("XZ")
    .center(0, TIE_HOLE_R)
    .circle(TIE_HOLE_D / 2.0)
    .extrude(T, both=True)
)
body = body.cut(center_hole).cut(tie_hole)

# ---------------- slot through back half (y from 0 to +h) ----------------
slot_len = R + 2.0 - TIE_HOLE_R
slot = (
    cq.Workplane("XY")
    .box(SLOT_W, h + 1.0, slot_len, centered=(True, False, False))
    .translate((0, 0, TIE_HOLE_R))
)
body = body.cut(slot)


# ---------------- cross recess on back face ----------------
def arm_wire(angle_deg):
    """Tapered arm from the centre, rounded tip; in local (u,v) then rotated."""
    a = CROSS_BASE_HW
    b = CROSS_TIP_R
    D = CROSS_L - b
    s = (a - b) / D
    c = math.sqrt(1 - s * s)
    p0u = (a * s, a * c)
    p1u = (D + b * s, b * c)
    p1l = (D + b * s, -b * c)
    p0l = (a * s, -a * c)
    tip = (D + b, 0.0)
    back = (-a, 0.0)
    th = math.radians(angle_deg)

    def rot(p):
        return (p[0] * math.cos(th) - p[1] * math.sin(th),
                p[0] * math.sin(th) + p[1] * math.cos(th))

    # workplane on the back face: local x = world X, local y = world Z
    wp = cq.Workplane("XZ", origin=(0, h, 0))
    w = (
        wp.moveTo(*rot(p0u))
        .lineTo(*rot(p1u))
        .threePointArc(rot(tip), rot(p1l))
        .lineTo(*rot(p0l))
        .threePointArc(rot(back), rot(p0u))
        .close()
    )
    # XZ workplane normal is -Y; extrude towards -Y (into the part)
    return w.extrude(CROSS_DEPTH)


cross = None
for i in range(4):
    arm = arm_wire(CROSS_ANGLE0 + 90.0 * i)
    cross = arm if cross is None else cross.union(arm)

body = body.cut(cross)

# round the concave corners between neighbouring cross arms
def _cross_corner(e):
    if not isinstance(e, cq.Edge) or e.geomType() != "LINE":
        return False
    c = e.Center()
    d = e.tangentAt(0.5)
    if abs(abs(d.y) - 1.0) > 1e-6:
        return False
    if not (h - CROSS_DEPTH - 0.01 < c.y < h + 0.01):
        return False
    # concave corners sit on the bisectors between neighbouring arms
    ang = math.degrees(math.atan2(c.z, c.x)) - (CROSS_ANGLE0 + 45.0)
    off = (ang + 45.0) % 90.0 - 45.0
    on_bisector = abs(off) < 0.5
    return on_bisector and math.hypot(c.x, c.z) < CROSS_L * 0.6


corner_edges = [e for e in body.edges().vals() if _cross_corner(e)]
body = _safe_fillet(body, corner_edges, CROSS_CORNER_FIL)

# soften the edges where the string slot breaks through the back flange
def _slot_edge(e):
    if not isinstance(e, cq.Edge):
        return False
    c = e.Center()
    if abs(abs(c.x) - SLOT_W / 2.0) > 1e-3:
        return False
    if c.y < 0.05:
        return False          # slot floor edge stays sharp
    if e.geomType() == "LINE" and abs(abs(e.tangentAt(0.5).y) - 1.0) < 1e-6:
        return False          # wall / tie-hole intersection stays sharp
    return True


slot_edges = [e for e in body.edges().vals() if _slot_edge(e)]
body = _safe_fillet(body, slot_edges, SLOT_FIL)

result = body
